import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
L = 120.0        # overall bar length (X)
D = 23.0         # top plate depth (Y), back face at Y=0, front edge at Y=-D
YB = 17.2        # depth of the body below the plate (front face at Y=-YB)
H = 15.6         # overall bar height (top at Z=0, bottom at Z=-H)
TP = 1.2         # top plate thickness (front overhang)
CH = 6.3         # 45 deg chamfer on the two front corners
N_CUP = 5
PITCH = 21.4
R1 = 9.72        # upper cup radius
Y_CUP = -13.3    # cup axis Y
Y_CHORD = -19.2  # straight front chord of the D shaped openings in the plate
Z_COVE = -9.4    # where the upper wall starts to roll inward (cove)
R_COVE = 9.02    # radius at the end of the cove (= radius of the short band)
Z_BAND = -11.2   # end of the cove / top of the short cylindrical band
Z_CONE = -12.4   # bottom of the band / top of the conical step
R2 = 7.45        # lower bore radius
Z2 = -13.8       # bottom of the conical step

NW = 5.7         # end notch width (X)
NH = 3.2         # end notch height (Z)
NOTCH_HOLE_D = 2.6
CB = 3.0         # back bottom chamfer

# central clip / mounting foot (profile in the YZ plane)
TC = 5.8         # clip thickness (X)
Y_CLIP = -11.5   # symmetry plane of the clip
C_OUT = 12.1     # outer face of the two columns (half span)
C_IN = 8.7       # inner face of the columns
EAR = 0.85       # ear height above plate top
Z_WING = -4.9    # where the wing slope starts at the column
TIP = 33.8       # wing tip half span
Z_TIP = -12.7    # top of the wing tip
Z_FOOT = -16.3   # underside of the wing feet
D_KINK = 17.3
D_KINK2 = 14.5
Z_INNER = -13.3  # underside of the clip between the feet
Z_WEB = -10.2    # top of the web crossing the middle cup
PIN_D = 2.1         # pin hole through the web
PIN_CB_D = 3.2      # counterbore on the underside of the web
PIN_CB_H = 1.0
EAR_R = 0.6         # rounding of the ear tops
TIP_R = 1.3         # rounding of the upper wing tip edge

# ---------------- body + plate ----------------
body = cq.Workplane("XY").box(L, YB, H, centered=(True, False, False)).translate((0, -YB, -H))
plate = cq.Workplane("XY").box(L, D, TP, centered=(True, False, False)).translate((0, -D, -TP))
part = body.union(plate)

# back-bottom chamfer along the full length
cham = (cq.Workplane("YZ").polyline([(0.01, -H - 0.01), (-CB, -H - 0.01), (0.01, -H + CB)]).close()
        .extrude(L + 2).translate((-L / 2 - 1, 0, 0)))
part = part.cut(cham)

# end notches (bottom of both ends) with a small hole in the ceiling
for sx in (-1, 1):
    notch = (cq.Workplane("XY").box(NW + 1, D + 2, NH + 1, centered=(False, False, False))
             .translate((L / 2 - NW, -D - 1, -H - 1)))
    if sx < 0:
        notch = notch.mirror("YZ")
    part = part.cut(notch)
    hole = (cq.Workplane("XY").circle(NOTCH_HOLE_D / 2).extrude(3.0)
            .translate((sx * (L / 2 - NW / 2), -YB / 2, -H + NH - 0.01)))
    part = part.cut(hole)

# cups: revolved stepped bore, D shaped in the plate
# upper wall + cove as one smooth curve: vertical down to about Z_COVE, then
# rolling inward to the band radius, meeting it at 45 deg
_z_top = 1.0
cup_sk = (cq.Workplane("XZ").moveTo(0, _z_top).lineTo(R1, _z_top)
          .spline([(R1 - 0.02, Z_COVE + 0.8), (R1 - 0.22, Z_COVE - 0.9), (R_COVE, Z_BAND)],
                  tangents=[(0, -1), (-1, -1)], includeCurrent=True)
          .lineTo(R_COVE, Z_CONE).lineTo(R2, Z2).lineTo(R2, -H - 1).lineTo(0, -H - 1).close())
cup_solid = cup_sk.revolve(360, (0, 0, 0), (0, 1, 0))
limit = cq.Workplane("XY").box(2 * R1 + 4, 30, H + 4, centered=(True, False, False)).translate((0, Y_CHORD, -H - 2))
for i in range(N_CUP):
    x = (i - (N_CUP - 1) / 2) * PITCH
    c = cup_solid.translate((x, Y_CUP, 0)).intersect(limit.translate((x, 0, 0)))
    part = part.cut(c)

# ---------------- central clip ----------------
pts = [(-C_OUT, EAR), (-C_OUT, Z_WING), (-TIP, Z_TIP), (-TIP, Z_FOOT), (-D_KINK, Z_FOOT),
       (-D_KINK2, Z_INNER), (D_KINK2, Z_INNER), (D_KINK, Z_FOOT), (TIP, Z_FOOT), (TIP, Z_TIP),
       (C_OUT, Z_WING), (C_OUT, EAR), (C_IN, EAR), (C_IN, Z_WEB), (-C_IN, Z_WEB), (-C_IN, EAR)]
clip = (cq.Workplane("YZ").polyline([(Y_CLIP + p[0], p[1]) for p in pts]).close()
        .extrude(TC).translate((-TC / 2, 0, 0)))


def fillet_at(wp, pts_yz, r):
    sel = [e for e in wp.edges("|X").vals()
           if any(abs(e.Center().y - py) < 0.05 and abs(e.Center().z - pz) < 0.05 for (py, pz) in pts_yz)]
    return wp.newObject(sel).fillet(r)


ears = [(Y_CLIP + s_ * d_, EAR) for s_ in (-1, 1) for d_ in (C_OUT, C_IN)]
clip = fillet_at(clip, ears, EAR_R)
clip = fillet_at(clip, [(Y_CLIP - C_OUT, Z_WING), (Y_CLIP + C_OUT, Z_WING)], 1.0)
clip = fillet_at(clip, [(Y_CLIP - TIP, Z_TIP), (Y_CLIP + TIP, Z_TIP)], TIP_R)
clip = fillet_at(clip, [(Y_CLIP - TIP, Z_FOOT), (Y_CLIP + TIP, Z_FOOT)], 0.3)
part = part.union(clip)

# pin hole through the web in the middle cup
pin = cq.Workplane("XY").circle(PIN_D / 2).extrude(H).translate((0, Y_CLIP, -H))
part = part.cut(pin)
pin_cb = cq.Workplane("XY").circle(PIN_CB_D / 2).extrude(PIN_CB_H + 1).translate((0, Y_CLIP, Z_INNER - 1))
part = part.cut(pin_cb)

# front corner chamfers (vertical planes through plate and body)
for sx in (-1, 1):
    tri = (cq.Workplane("XY").polyline([(L / 2 + 1, -D + CH + 1), (L / 2 + 1, -D - 5), (L / 2 - CH - 5, -D - 5)])
           .close().extrude(H + 4).translate((0, 0, -H - 2)))
    if sx < 0:
        tri = tri.mirror("YZ")
    part = part.cut(tri)

result = part
